import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_TOT = 150.0      # overall length incl. nose tab (X)
L_BODY = 139.8     # channel length on the +Y side (end of back wall)
X_CH = 124.1       # start of the front (-Y) nose chamfer
W = 44.6           # overall width (Y)
H = 22.0           # overall height (Z)
T_PLATE = 7.4      # top plate thickness
T_WALL = 4.4       # side wall thickness
R_IN = 7.3         # inner fillet plate/wall
TAB_HW = 6.9       # half width of the nose tab
NOTCH_D = 8.9      # depth of the step on the +Y side of the nose

HEX_D = 9.1        # hex hole, across corners (corners point along Y)
PITCH = 12.0       # hex hole pitch (X and Y)
X_MID = 69.9       # centre of hole pattern / emblem
GROUP_OFF = 24.2   # distance from X_MID to the first column of each group

EMB_APO = 14.0      # emblem hexagon ring, centre-line apothem
SLOT_W = 2.2        # emblem slot width
EMB_GAP = 2.5       # gap at the hexagon corners
DIAG_ANG = 52.5     # inclination of inner slash slots (deg from X)
DIAG_H = 7.6        # half height of the long slash
DIAG_OFF = 6.4      # horizontal offset of the short slashes
DIAG_WX = 2.7      # horizontal width of the slash slots

HOLE_D = 5.0        # cross holes in the side walls
HOLE_X = (21.5, 126.6)
HOLE_Z = 11.0
CB_D = 7.0          # spot-face counterbore on the inside of the walls
CB_DEPTH = 1.5      # depth of the spot face below the inner wall plane
CB_SIDES = (1.0,)   # spot faces only on the back (+Y) wall

CH_TOP = 0.6        # small chamfer on top outline edges
R_V_FRONT = 6.5     # vertical round where the side face meets the nose chamfer
R_V_TAB = 1.2       # vertical round nose chamfer -> tab end
R_END = 0.8         # round on the lower edges of the wall end faces
R_FOOT = 2.4        # round on the inner bottom edge of the side walls
R_END_CORNER = 2.8  # rounded lower inner corner of the front wall end face

hw = W / 2.0
zi = H - T_PLATE


# ---------------- U channel profile (YZ), extruded along X ----------------
def u_profile():
    c = math.cos(math.radians(45))
    a = hw - T_WALL
    R = R_IN
    wp = (
        cq.Workplane("YZ")
        .moveTo(-hw, 0)
        .lineTo(-a, 0)
        .lineTo(-a, zi - R)
        .threePointArc((-a + R - R * c, zi - R + R * c), (-a + R, zi))
        .lineTo(a - R, zi)
        .threePointArc((a - R + R * c, zi - R + R * c), (a, zi - R))
        .lineTo(a, 0)
        .lineTo(hw, 0)
        .lineTo(hw, H)
        .lineTo(-hw, H)
        .close()
    )
    return wp


body = u_profile().extrude(L_TOT)

# ---------------- plan outline (nose) ----------------
outline_pts = [
    (0.0, -hw),
    (X_CH, -hw),
    (L_TOT, -TAB_HW),
    (L_TOT, TAB_HW),
    (L_BODY, hw - NOTCH_D),
    (L_BODY, hw),
    (0.0, hw),
]
outline = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .polyline(outline_pts)
    .close()
    .extrude(H + 2.0)
)


def vsel(x, y, tol=0.05):
    return cq.selectors.BoxSelector((x - tol, y - tol, -5), (x + tol, y + tol, H + 5))


# round the vertical corners of the plan outline
for (px, py, rr) in (
    (X_CH, -hw, R_V_FRONT),
    (L_TOT, -TAB_HW, R_V_TAB),
):
    outline = outline.edges(vsel(px, py)).fillet(rr)

body = body.intersect(outline)

# small chamfer all round the top outline
body = body.faces(">Z").edges().chamfer(CH_TOP)


# round the lower edges of the wall end faces (nose chamfer plane / back wall end)
def _edges_on_plane(shape, p0, n, zmax, tol=1e-3):
    p0 = cq.Vector(*p0)
    n = cq.Vector(*n).normalized()
    out = []
    for e in shape.Edges():
        pts = [e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0)]
        if all(abs((p - p0).dot(n)) < tol for p in pts) and max(p.z for p in pts) < zmax:
            out.append(e)
    return out


_ch_dir = cq.Vector(L_TOT - X_CH, -TAB_HW + hw, 0).normalized()
_ch_n = cq.Vector(_ch_dir.y, -_ch_dir.x, 0.0)   # outward normal of the nose chamfer


def round_end_face(shape_wp, p0, n, zmax, r):
    sel = _edges_on_plane(shape_wp.val(), p0, n, zmax)
    try:
        return shape_wp.newObject(sel).fillet(r)
    except Exception:
        return shape_wp


# 1) front wall end (on the nose chamfer plane)
body = round_end_face(body, (X_CH, -hw, 0.0), _ch_n.toTuple(), zi + 0.01, R_END)


# 2) round on the inner bottom edges of the side walls (cut a fillet sliver)
def foot_sliver(sgn):
    a = hw - T_WALL
    r = R_FOOT
    c = math.cos(math.radians(45))
    # in (Y, Z) for the -Y wall, mirrored (sgn=-1) for the +Y wall
    mid = (-a - r + r * c, r - r * c)
    end = (-a - r, 0.0)
    wp = (
        cq.Workplane("YZ")
        .workplane(offset=-1.0)
        .moveTo(sgn * (-a + 0.2), -0.2)
        .lineTo(sgn * (-a + 0.2), r)
        .lineTo(sgn * (-a), r)
        .threePointArc((sgn * mid[0], mid[1]), (sgn * end[0], end[1]))
        .lineTo(sgn * end[0], -0.2)
        .close()
        .extrude(L_TOT + 2.0)
    )
    return wp


for _s in (1.0, -1.0):
    body = body.cut(foot_sliver(_s))

# 3) back wall end and rear end of the channel
body = round_end_face(body, (L_BODY, 0.0, 0.0), (1.0, 0.0, 0.0), zi + 0.01, R_END)
body = round_end_face(body, (0.0, 0.0, 0.0), (1.0, 0.0, 0.0), zi + 0.01, R_END)

# the end round on the front wall propagates along its outer bottom edge;
# give the back wall the same outer bottom round
_sel = [
    e for e in body.val().Edges()
    if e.geomType() == "LINE"
    and all(abs(e.positionAt(t).z) < 1e-4 and abs(e.positionAt(t).y - hw) < 1e-3 for t in (0.0, 1.0))
]
try:
    body = body.newObject(_sel).fillet(R_END)
except Exception:
    pass

# 4) rounded lower inner corner of the front wall end face (in the chamfer plane)
_th = math.atan2(hw - TAB_HW, L_TOT - X_CH)
_s_edge = T_WALL / math.sin(_th)                       # sharp inner edge
_s_t = _s_edge - R_END / math.tan(_th / 2.0)           # tangent line of the end round
_rho = R_END_CORNER
_c45 = math.cos(math.radians(45))
_pl = cq.Plane(
    origin=(cq.Vector(X_CH, -hw, 0.0) + _ch_n * 0.5).toTuple(),
    xDir=_ch_dir.toTuple(),
    normal=_ch_n.toTuple(),
)
_corner_cut = (
    cq.Workplane(_pl)
    .moveTo(_s_t - _rho, -1.0)
    .lineTo(_s_edge + 1.0, -1.0)
    .lineTo(_s_edge + 1.0, _rho)
    .lineTo(_s_t, _rho)
    .threePointArc((_s_t - _rho + _rho * _c45, _rho - _rho * _c45), (_s_t - _rho, 0.0))
    .close()
    .extrude(-6.0)
)
body = body.cut(_corner_cut)

# ---------------- hex holes ----------------
def hex_pts(cx, cy, d):
    r = d / 2.0
    return [
        (cx + r * math.cos(math.radians(90 + 60 * k)),
         cy + r * math.sin(math.radians(90 + 60 * k)))
        for k in range(6)
    ]


hole_centres = []
for side in (-1, 1):
    for i in range(4):
        x = X_MID + side * (GROUP_OFF + i * PITCH)
        hole_centres.append((x, 0.0))
        if i < 3:
            hole_centres.append((x, PITCH))
            hole_centres.append((x, -PITCH))

cutter = None
for (cx, cy) in hole_centres:
    p = (
        cq.Workplane("XY")
        .workplane(offset=-1.0)
        .polyline(hex_pts(cx, cy, HEX_D))
        .close()
        .extrude(H + 2.0)
    )
    cutter = p if cutter is None else cutter.union(p)

# ---------------- emblem: segmented hexagon ring + slashes ----------------
def ring_slot(k, a_in, a_out, gap):
    t1 = math.radians(90 + 60 * k)
    t2 = t1 + math.radians(60)
    u1 = (math.cos(t1), math.sin(t1))
    u2 = (math.cos(t2), math.sin(t2))
    w1 = (-u1[1], u1[0])      # rotate +90
    w2 = (u2[1], -u2[0])      # rotate -90
    g = gap / 2.0

    def q(u, w, a):
        s = (a - 0.5 * g) / math.cos(math.radians(30))
        return (X_MID + s * u[0] + g * w[0], s * u[1] + g * w[1])

    return [q(u1, w1, a_in), q(u1, w1, a_out), q(u2, w2, a_out), q(u2, w2, a_in)]


emb_polys = []
for k in range(6):
    emb_polys.append(ring_slot(k, EMB_APO - SLOT_W / 2.0, EMB_APO + SLOT_W / 2.0, EMB_GAP))

dx_full = DIAG_H / math.tan(math.radians(DIAG_ANG))


def slash(ax, ay, bx, by):
    h = DIAG_WX / 2.0
    return [
        (X_MID + ax - h, ay),
        (X_MID + ax + h, ay),
        (X_MID + bx + h, by),
        (X_MID + bx - h, by),
    ]


emb_polys.append(slash(-dx_full, -DIAG_H, dx_full, DIAG_H))
emb_polys.append(slash(-DIAG_OFF, 0.0, -DIAG_OFF + dx_full, DIAG_H))
emb_polys.append(slash(DIAG_OFF - dx_full, -DIAG_H, DIAG_OFF, 0.0))

for pts in emb_polys:
    p = (
        cq.Workplane("XY")
        .workplane(offset=-1.0)
        .polyline(pts)
        .close()
        .extrude(H + 2.0)
    )
    cutter = cutter.union(p)

body = body.cut(cutter)

# ---------------- cross holes through the side walls ----------------
for hx in HOLE_X:
    cyl = cq.Workplane("XY").add(
        cq.Solid.makeCylinder(
            HOLE_D / 2.0, W + 4.0,
            cq.Vector(hx, -hw - 2.0, HOLE_Z), cq.Vector(0, 1, 0)
        )
    )
    body = body.cut(cyl)
    for sgn in CB_SIDES:
        y_floor = sgn * (hw - T_WALL + CB_DEPTH)
        length = CB_DEPTH + R_IN + 0.5
        cb = cq.Workplane("XY").add(
            cq.Solid.makeCylinder(
                CB_D / 2.0, length,
                cq.Vector(hx, y_floor, HOLE_Z), cq.Vector(0, -sgn, 0)
            )
        )
        body = body.cut(cb)

result = body
